import math
import cadquery as cq

# Round cover plate: flat back, front face with a drafted lobed pocket,
# eight D-shaped screw bosses on the rim, four of them drilled through.
VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
R_OUT = 100.0          # outer radius of the cover disc
T = 10.0               # disc thickness (back face at Y=0, rim face at Y=-T)
EDGE_R = 1.0           # small round on the front outer edge

POCKET_D = 7.2         # pocket depth below the rim face
WALL_TAPER = 34.0      # pocket wall draft, measured from the pocket axis (deg)
R_FLOOR = 90.1         # radius of the floor edge along the plain arcs
N_BOSS = 8
R_BOSS = 88.0          # boss pitch radius
LOBE_FLOOR_R = 16.5    # floor-edge radius of the lobe left around each boss
CORNER_R = 5.0         # floor-level rounding where a lobe meets an outer arc
STRAIGHT_SEG = 3       # the wall between boss 3 (135 deg) and boss 4 (180 deg) is straight

D_R = 9.0              # D-shaped boss radius
D_FLAT = 6.8           # boss centre to the flat (flat faces radially outward)
D_H = 2.0              # D boss height above the rim face
CB_R = 5.5             # counterbore radius in each boss
CB_D = 2.5             # counterbore depth from the boss top
CSK_R = 3.6            # countersink at the counterbore floor (top radius)
SLOT_W = 1.2           # three small radial slots around each counterbore
SLOT_R1 = 7.8          # slots run from the counterbore out to this radius
SLOT_D = 1.5           # slot depth from the boss top
HOLE_R = 2.5           # through hole (only in the 4 bosses on the axes)


# ---------------- helpers ----------------
def boss_angle(i):
    return 2.0 * math.pi * i / N_BOSS


def pocket_outline(wp, ra, rl, rc):
    """Closed outline: circle ra minus lobe circles rl at every boss, with
    rounds rc where a lobe meets the outer boundary.  The segment after boss
    STRAIGHT_SEG is a straight line tangent to circle ra at its middle.
    Drawn on a workplane whose local x,y are global X,Z."""

    def pol(r, a):
        return (r * math.cos(a), r * math.sin(a))

    def rounds_circle(c, th, sgn):
        # round tangent to circle ra (inside) and lobe circle rl (outside)
        d = ra - rc
        cphi = (d * d + R_BOSS * R_BOSS - (rl + rc) ** 2) / (2.0 * d * R_BOSS)
        a = th + sgn * math.acos(cphi)
        return pol(d, a), pol(ra, a)

    def rounds_line(c, mid_a, sgn):
        # round tangent to the line {p . u = ra} and the lobe circle
        u = (math.cos(mid_a), math.sin(mid_a))
        v = (-u[1], u[0])
        cu = c[0] * u[0] + c[1] * u[1]
        cv = c[0] * v[0] + c[1] * v[1]
        t = cv - sgn * math.sqrt((rl + rc) ** 2 - (ra - rc - cu) ** 2)
        f = ((ra - rc) * u[0] + t * v[0], (ra - rc) * u[1] + t * v[1])
        to = (ra * u[0] + t * v[0], ra * u[1] + t * v[1])
        return f, to

    step = 2.0 * math.pi / N_BOSS
    segs = []
    for i in range(N_BOSS):
        th = boss_angle(i)
        c = pol(R_BOSS, th)
        items = []
        for sgn in (-1, 1):
            if sgn == 1 and i == STRAIGHT_SEG:
                f, to = rounds_line(c, th + step / 2.0, -1)
            elif sgn == -1 and (i - 1) % N_BOSS == STRAIGHT_SEG:
                f, to = rounds_line(c, th - step / 2.0, 1)
            else:
                f, to = rounds_circle(c, th, sgn)
            vx, vy = f[0] - c[0], f[1] - c[1]
            n = math.hypot(vx, vy)
            tl = (c[0] + rl * vx / n, c[1] + rl * vy / n)
            bx = (to[0] - f[0]) + (tl[0] - f[0])
            by = (to[1] - f[1]) + (tl[1] - f[1])
            bn = math.hypot(bx, by)
            fm = (f[0] + rc * bx / bn, f[1] + rc * by / bn)
            items.append((to, fm, tl))
        (to_m, fm_m, tl_m), (to_p, fm_p, tl_p) = items
        lobe_mid = pol(R_BOSS - rl, th)
        segs.append((to_m, fm_m, tl_m, lobe_mid, tl_p, fm_p, to_p))

    w = wp.moveTo(*segs[0][0])
    for i in range(N_BOSS):
        to_m, fm_m, tl_m, lobe_mid, tl_p, fm_p, to_p = segs[i]
        w = w.threePointArc(fm_m, tl_m)
        w = w.threePointArc(lobe_mid, tl_p)
        w = w.threePointArc(fm_p, to_p)
        nxt = segs[(i + 1) % N_BOSS][0]
        if i == STRAIGHT_SEG:
            w = w.lineTo(*nxt)
        else:
            w = w.threePointArc(pol(ra, boss_angle(i) + step / 2.0), nxt)
    return w.close()


def d_shape(wp, r, flat):
    # D profile in a local frame whose +x points radially outward
    h = math.sqrt(r * r - flat * flat)
    return wp.moveTo(flat, -h).threePointArc((-r, 0), (flat, h)).close()


# ---------------- base disc ----------------
# Workplane "XZ": local x = X, local y = Z, extrusion towards -Y.
body = cq.Workplane("XZ").circle(R_OUT).extrude(T)          # Y from 0 to -T
body = body.faces("<Y").edges().fillet(EDGE_R)

# ---------------- drafted pocket with boss lobes ----------------
EXTRA = 1.0
pocket = pocket_outline(
    cq.Workplane("XZ").workplane(offset=T - POCKET_D), R_FLOOR, LOBE_FLOOR_R, CORNER_R
).extrude(POCKET_D + EXTRA, taper=-WALL_TAPER)
body = body.cut(pocket)

# ---------------- D bosses with counterbores ----------------
for i in range(N_BOSS):
    a = boss_angle(i)
    x, z = R_BOSS * math.cos(a), R_BOSS * math.sin(a)
    # local frame: +x radially outward, +y tangential, extrusion towards -Y
    pl = cq.Plane(origin=(x, -T, z), xDir=(math.cos(a), 0, math.sin(a)), normal=(0, -1, 0))
    boss = d_shape(cq.Workplane(pl).workplane(offset=-0.5), D_R, D_FLAT).extrude(D_H + 0.5)
    body = body.union(boss)
    cb = cq.Workplane(pl).workplane(offset=D_H).circle(CB_R).extrude(-CB_D)
    body = body.cut(cb)
    # radial slots (inner side and both lateral sides)
    for ang in (90.0, 180.0, 270.0):
        slot = (cq.Workplane(pl).workplane(offset=D_H)
                .transformed(rotate=(0, 0, ang))
                .center((CB_R - 0.5 + SLOT_R1) / 2.0, 0)
                .rect(SLOT_R1 - CB_R + 0.5, SLOT_W)
                .extrude(-SLOT_D))
        body = body.cut(slot)
    # countersink cone at the counterbore floor, down to the hole radius
    csk = cq.Solid.makeCone(
        CSK_R, HOLE_R, CSK_R - HOLE_R,
        pnt=cq.Vector(x, -T - D_H + CB_D - 0.01, z), dir=cq.Vector(0, 1, 0),
    )
    body = body.cut(cq.Workplane().add(csk))
    if i % 2 == 0:
        hole = cq.Workplane(pl).workplane(offset=D_H).circle(HOLE_R).extrude(-(T + D_H + 1))
        body = body.cut(hole)

result = body
